import math
import cadquery as cq

# ---------------------------------------------------------------
# Driving dimensions (mm).  X: plate thickness / foot direction,
# Y: width (symmetric), Z: height.  Front face of the plate at X=0.
# ---------------------------------------------------------------
T = 15.4            # plate thickness (X from -T to 0)
HW = 20.3           # half width of the main body (full thickness)
HW_UP = 24.4        # half width of the widened upper front frame
Z_TAPER0 = 74.25    # start of the widening taper
Z_TAPER1 = 86.75    # end of the widening taper
Y_HORN = 19.0       # horn ridge half spacing
Z_TOP = 118.75      # overall height (horn tips)
FRAME_T = 10.9      # thickness of the lugs (flush with the front face)
TAPER_T = 7.25      # thickness of the widened front frame (taper, upper part)

LUG_Y = 25.3        # lug hole offset from centre line
LUG_Z = (18.6, 96.1)
LUG_R = 6.9         # lug outer radius
HOLE_R = 4.05       # lug hole radius
LUG_FILLET_BOT = 5.0
LUG_FILLET_TOP = 2.5

# top profile (side view): sloped line then round into the back face
SLOPE = 0.358                     # dZ/dX of the sloped top
SLOPE_X = -11.2                   # end of the straight slope
TOP_BACK_Z = 108.75               # top of the back face (round is tangent)
CHAMFER = 0.85                     # horn outer chamfer (dZ/dY)

# rounded cup forming the top (vertical cylinder around the top pocket)
CUP_XC = 9.2
CUP_R = 26.1
CUP_Z0 = 104.0      # cup wall is a plain cylinder above this height
CUP_FLARE = 7.0     # 45 deg flare below CUP_Z0 blending into the lugs/body

# U saddle across the top (cylinder along X)
U_R = 22.4
U_ZC = 108.2 + U_R

# top pocket (vertical cylinder opening to the front, two levels)
TP_XC = 10.3
TP_R = 21.7
TP_HW_UP = 18.95
TP_Z_UP = 102.4
TP_CH_Z = 112.45    # top corners of the upper pocket are chamfered
TP_CH_SLOPE = 0.673 # chamfer dZ/dY
TP_HW_LO = 15.6
TP_Z_LO = 95.85

# main cavity
CAV_HW = 15.75
RECT_DEPTH = 9.1
RECT_Z0 = 62.9
RECT_Z1 = 91.1
CYL_XC = 5.9
CYL_R = math.hypot(CYL_XC, CAV_HW)

# flat side pocket in the cylindrical cavity (+Y side only)
SIDE_P_Y0 = 0.0
SIDE_P_Z0, SIDE_P_Z1 = 48.3, 55.0
SIDE_HOLE_R = 1.3
SIDE_HOLE_Y = 15.0

# foot
FOOT_L = 33.0
FOOT_T = 6.5
FOOT_R = 3.4
FOOT_EDGE_R = 0.8

# tab (latch hook at the top of the cavity)
TAB_BASE_HW = 6.66
TAB_X1 = 3.4
TAB_X2 = 5.1
TAB_TIP_HW = 4.27
TAB_NOTCH_XC = 10.0
TAB_NOTCH_R = 6.5

# slots
TOP_SLOT_Y0, TOP_SLOT_Y1 = 4.6, 13.9
TOP_SLOT_Z0, TOP_SLOT_Z1 = 100.1, 102.1
BOT_SLOT_Y0, BOT_SLOT_Y1 = 9.4, 12.6
BOT_SLOT_Z1 = 16.0
SHELF_SLOT_HW = 4.0
SHELF_SLOT_X0 = -12.4
SHELF_SLOT_D = 1.2

# bottom hook block
BLK_X = -4.3
BLK_HW = 5.6
BLK_Z1 = 15.7

# back recessed panel
PANEL_HW = 17.0
PANEL_Z0, PANEL_Z1 = 25.0, 75.0
PANEL_D = 1.0

# back grooves (top: three T-shaped grooves under the slots, bottom: along the slots)
GROOVE_W = 1.6
GROOVE_D = 1.0
TOP_GROOVE_Y = (-9.25, 0.0, 9.25)
MID_BAR_HW = 3.5
MID_BAR_Z0, MID_BAR_Z1 = 96.5, 98.5
TOP_GROOVE_Z0 = PANEL_Z1 + 1.5
BOT_GROOVE_Z0 = 2.0
BOT_GROOVE_D = 2.5


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def zcyl(xc, yc, r, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center(xc, yc).circle(r).extrude(z1 - z0))


def half_space(point, normal, size=400.0):
    """big slab on the +normal side of the plane through point"""
    n = cq.Vector(*normal).normalized()
    xd = n.cross(cq.Vector(0, 0, 1))
    if xd.Length < 1e-6:
        xd = cq.Vector(1, 0, 0)
    pl = cq.Plane(origin=cq.Vector(*point), xDir=xd.normalized(), normal=n)
    return cq.Workplane(pl).rect(size, size).extrude(size / 2)


class _Near(cq.Selector):
    """select sketch vertices close to given (u, v) points"""

    def __init__(self, pts, tol=0.8):
        self.pts = pts
        self.tol = tol

    def filter(self, objs):
        return [o for o in objs
                if any(abs(o.Center().x - p[0]) < self.tol and
                       abs(o.Center().y - p[1]) < self.tol for p in self.pts)]


# ---------------- body ----------------
ZH = Z_TOP + 5.0   # build tall, shape the top by cuts
lug_pts = [(sy * LUG_Y, z) for sy in (-1, 1) for z in LUG_Z]

# full-thickness core
core_half = [(HW, 0), (HW, ZH)]
core_pts = [(-y, z) for (y, z) in reversed(core_half)] + core_half
body = (cq.Workplane("YZ").workplane(offset=-T)
        .polyline(core_pts).close().extrude(T))

bot_lugs = [p for p in lug_pts if p[1] < 50]
top_lugs = [p for p in lug_pts if p[1] >= 50]


def _lug_junctions(sk, centres):
    verts = [(v.X, v.Y) for v in sk._faces.Vertices()]
    return [p for p in verts
            if any(abs(math.hypot(p[0] - c[0], p[1] - c[1]) - LUG_R) < 0.05
                   for c in centres)]


# lower lugs, blended into the core with generous fillets (lug thickness)
skb = cq.Sketch().polygon([(-HW, 0), (HW, 0), (HW, 50), (-HW, 50), (-HW, 0)])
skb = skb.push(bot_lugs).circle(LUG_R, mode="a").reset().clean()
skb = skb.vertices(_Near(_lug_junctions(skb, bot_lugs))).fillet(LUG_FILLET_BOT).reset()
LUG_BACK_FILLET = 4.4
LUG_BACK_FILLET_TOP = 2.0
lower = (box(-T, 0, -HW, HW, 0, 50)
         .union(cq.Workplane("YZ").workplane(offset=-FRAME_T)
                .placeSketch(skb).extrude(FRAME_T)))
lower = (lower.edges("|Z")
         .edges(cq.selectors.BoxSelector((-FRAME_T - 0.1, -HW - 0.1, 0),
                                         (-FRAME_T + 0.1, HW + 0.1, 50)))
         .fillet(LUG_BACK_FILLET))
body = body.union(lower)

# upper front frame: taper, widening and the upper lugs (front outline)
_k = (HW_UP - HW) / (Z_TAPER1 - Z_TAPER0)
_tz = LUG_Z[1] - 6.6
fr_half = [(HW - 0.01, 50), (HW, Z_TAPER0), (HW + _k * (_tz - Z_TAPER0), _tz),
           (HW_UP, LUG_Z[1]), (HW_UP, ZH)]
fr_pts = [(-y, z) for (y, z) in reversed(fr_half)] + fr_half
sk = cq.Sketch().polygon(fr_pts + [fr_pts[0]])
sk = sk.push(top_lugs).circle(LUG_R, mode="a").reset().clean()
sk = sk.vertices(_Near(_lug_junctions(sk, top_lugs))).fillet(LUG_FILLET_TOP).reset()
sk = sk.vertices(_Near([(HW, Z_TAPER0), (-HW, Z_TAPER0)])).fillet(6.0).reset()
frame = (cq.Workplane("YZ").workplane(offset=-TAPER_T)
         .placeSketch(sk).extrude(TAPER_T))
# the taper is a ruled wedge running back into the core side at X=-TAPER_T
_zt = LUG_Z[1] - 7.6
_wt = HW + _k * (_zt - Z_TAPER0)
for sy in (-1, 1):
    fw = [(sy * HW, 60), (sy * HW, Z_TAPER0 - 0.95),
          (sy * (HW + 0.3), Z_TAPER0 + 0.93), (sy * _wt, _zt),
          (sy * 40, _zt), (sy * 40, 60)]
    bw = [(sy * (HW - 0.1), 60), (sy * (HW - 0.1), Z_TAPER0 - 0.95),
          (sy * (HW - 0.1), Z_TAPER0 + 0.93), (sy * (HW - 0.1), _zt),
          (sy * 40, _zt), (sy * 40, 60)]
    w_front = cq.Workplane("YZ").workplane(offset=0.5).polyline(fw).close().wires().val()
    w_back = (cq.Workplane("YZ").workplane(offset=-TAPER_T - 0.05)
              .polyline(bw).close().wires().val())
    frame = frame.cut(cq.Workplane("XY").add(
        cq.Solid.makeLoft([w_front, w_back], True)))
body = body.union(frame)
# upper lugs and the head above them at full lug thickness
body = body.union(cq.Workplane("YZ").workplane(offset=-FRAME_T)
                  .pushPoints(top_lugs).circle(LUG_R).extrude(FRAME_T))
body = body.union(box(-FRAME_T, 0, -HW_UP, HW_UP, LUG_Z[1], ZH))

# round the inside corners between the back of the upper lugs and the core
body = (body.edges("|Z")
        .edges(cq.selectors.BoxSelector((-FRAME_T - 0.1, -HW - 0.1, 55),
                                        (-FRAME_T + 0.1, HW + 0.1, ZH + 1)))
        .fillet(LUG_BACK_FILLET_TOP))

# ---------------- top shaping ----------------
# rounded cup above the lugs
cup_solid = (cq.Workplane("XY").workplane(offset=CUP_Z0 - CUP_FLARE)
             .center(CUP_XC, 0).circle(CUP_R + CUP_FLARE)
             .workplane(offset=CUP_FLARE).circle(CUP_R).loft()
             .union(zcyl(CUP_XC, 0, CUP_R, CUP_Z0, ZH + 10)))
outside_cup = (box(-T - 5, 30, -40, 40, CUP_Z0 - CUP_FLARE, ZH + 5)
               .cut(cup_solid)
               .cut(cq.Workplane("YZ").workplane(offset=-FRAME_T)
                    .pushPoints(top_lugs).circle(LUG_R).extrude(FRAME_T + 5)))
body = body.cut(outside_cup)

# sloped top (side view profile)
slope_z = Z_TOP + SLOPE * SLOPE_X
slope_cut = (cq.Workplane("XZ")
             .moveTo(5, Z_TOP + 5 * SLOPE).lineTo(SLOPE_X, slope_z)
             .tangentArcPoint((-T, TOP_BACK_Z), relative=False)
             .lineTo(-T, TOP_BACK_Z - 3).lineTo(-T - 3, TOP_BACK_Z - 3)
             .lineTo(-T - 3, 150).lineTo(5, 150)
             .close().extrude(60, both=True))
body = body.cut(slope_cut)

# 45 degree outer chamfers of the horns, following the slope
for sy in (-1, 1):
    body = body.cut(half_space((0, sy * Y_HORN, Z_TOP),
                               (-SLOPE, sy * CHAMFER, 1.0)))

# U saddle
u_cut = (cq.Workplane("YZ").workplane(offset=-T - 5)
         .center(0, U_ZC).circle(U_R).extrude(T + 10))
body = body.cut(u_cut)

# top pocket (two stepped levels)
_apex = TP_CH_Z + TP_HW_UP * TP_CH_SLOPE
tp_prof = (cq.Workplane("YZ").workplane(offset=-T - 5)
           .polyline([(-TP_HW_UP, TP_Z_UP), (TP_HW_UP, TP_Z_UP),
                      (TP_HW_UP, TP_CH_Z), (0, _apex), (-TP_HW_UP, TP_CH_Z)])
           .close().extrude(T + 40))
tp = zcyl(TP_XC, 0, TP_R, TP_Z_UP, 150).intersect(tp_prof)
tp2 = zcyl(TP_XC, 0, TP_R, TP_Z_LO, 150).intersect(
    box(-T, 40, -TP_HW_LO, TP_HW_LO, TP_Z_LO, 150))
body = body.cut(tp).cut(tp2)

# ---------------- main cavity ----------------
body = body.cut(box(-RECT_DEPTH, 1, -CAV_HW, CAV_HW, RECT_Z0, RECT_Z1))
body = body.cut(zcyl(CYL_XC, 0, CYL_R, FOOT_T, RECT_Z0))
body = body.cut(box(-RECT_DEPTH, 1, SIDE_P_Y0, CAV_HW, SIDE_P_Z0, SIDE_P_Z1))
body = body.cut(cq.Workplane("YZ").workplane(offset=-T - 1)
                .center(SIDE_HOLE_Y, (SIDE_P_Z0 + SIDE_P_Z1) / 2)
                .circle(SIDE_HOLE_R).extrude(T + 1 - RECT_DEPTH + 0.01))

# ---------------- foot ----------------
foot = (cq.Workplane("XY")
        .box(FOOT_L + T, 2 * HW, FOOT_T, centered=False)
        .translate((-T, -HW, 0))
        .edges("|Z and >X").fillet(FOOT_R))
body = body.union(foot)
# small chamfer all round the underside
body = body.faces("<Z").edges().chamfer(FOOT_EDGE_R)

# ---------------- bottom hook block ----------------
blk = box(-12.5, BLK_X, -BLK_HW, BLK_HW, FOOT_T - 0.5, BLK_Z1)
body = body.union(blk)

# ---------------- top tab ----------------
tab = (cq.Workplane("XY").workplane(offset=RECT_Z1)
       .moveTo(-1, -TAB_BASE_HW).lineTo(TAB_X1, -TAB_BASE_HW)
       .lineTo(TAB_X2, -TAB_TIP_HW)
       .threePointArc((TAB_NOTCH_XC - TAB_NOTCH_R, 0), (TAB_X2, TAB_TIP_HW))
       .lineTo(TAB_X1, TAB_BASE_HW).lineTo(-1, TAB_BASE_HW).close()
       .extrude(TP_Z_LO - RECT_Z1))
body = body.union(tab)

# ---------------- slots ----------------
for sy in (-1, 1):
    y0, y1 = sorted((sy * TOP_SLOT_Y0, sy * TOP_SLOT_Y1))
    body = body.cut(box(-T - 1, -5, y0, y1, TOP_SLOT_Z0, TOP_SLOT_Z1))
    y0, y1 = sorted((sy * BOT_SLOT_Y0, sy * BOT_SLOT_Y1))
    body = body.cut(box(-T - 1, 1, y0, y1, FOOT_T, BOT_SLOT_Z1))

body = body.cut(box(SHELF_SLOT_X0, 0, -SHELF_SLOT_HW, SHELF_SLOT_HW,
                    TP_Z_LO - SHELF_SLOT_D, TP_Z_LO + 2.0))

# ---------------- back grooves ----------------
body = body.cut(box(-T - 1, -T + GROOVE_D, -MID_BAR_HW, MID_BAR_HW,
                    MID_BAR_Z0, MID_BAR_Z1))
for gy in TOP_GROOVE_Y:
    gz1 = MID_BAR_Z1 if gy == 0 else TOP_SLOT_Z1
    body = body.cut(box(-T - 1, -T + GROOVE_D, gy - GROOVE_W / 2, gy + GROOVE_W / 2,
                        TOP_GROOVE_Z0, gz1))
for sy in (-1, 1):
    y0, y1 = sorted((sy * BOT_SLOT_Y0, sy * BOT_SLOT_Y1))
    body = body.cut(box(-T - 1, -T + BOT_GROOVE_D, y0, y1,
                        BOT_GROOVE_Z0, PANEL_Z0))

# ---------------- back recessed panel ----------------
body = body.cut(box(-T - 1, -T + PANEL_D, -PANEL_HW, PANEL_HW,
                    PANEL_Z0, PANEL_Z1))

# ---------------- lug holes ----------------
holes = (cq.Workplane("YZ").workplane(offset=-T - 5)
         .pushPoints(lug_pts).circle(HOLE_R).extrude(T + 10))
body = body.cut(holes)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
